import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
HW = 39.7          # half width (X)
YF = -59.45        # front face (Y)
YB = 43.6          # back end of the arms (Y)
H = 16.9           # overall height
T = 3.2            # top plate thickness
WT = 3.3           # side / front wall thickness
WT_BACK = 1.2      # back wall thickness of the two arms
R_FRONT = 6.4      # front top edge round
R_SIDE = 3.0       # side top edge round

# U cut-out (open to the back)
CUT_W = 21.95      # half width of the wide part of the window
CUT_N = 14.8       # half width of the narrow part / opening
CUT_Y0 = -1.45     # front end of the cut-out
LUG_F = 5.25       # front lugs end (Y)
LUG_B = 35.2       # back lugs start (Y)
LUG_R = 3.1        # lug inner corner round
LUG_HOLE = 2.7
LUG_HX = 18.6
LUG_HY = (1.9, 39.4)

# slots
SLOT_X = (-30.6, -10.25, 10.25, 30.6)
SLOT_W = 1.8
SLOT_Y1 = -17.4
FINGER_LIFT = 2.6

# right side notch / window
NOTCH_Y = (-26.2, -4.95)
WIN_Y = (5.85, 34.25)
WIN_Z = 11.65
WIN_Z_IN = 9.2     # window top slopes down towards the inside

# mounting tab at the back right
TAB_X0 = 26.65
TAB_YE = 59.45
TAB_T = 4.5
TAB_R = 8.3
TAB_HOLE = 4.4
TAB_CB = 9.6       # spot face around the tab hole
R_TAB = 1.2        # round along the outer edge of the tab sweep
R_TAB_END = 1.0    # round on the vertical end corners of the tab
TAB_HX, TAB_HY = 30.7, 52.35

# screw blocks in the two front corners: a gusset with a sloped top that
# grows out of the side wall / ceiling, with a vertical screw hole
GB_Y = (-54.5, -44.8)  # gusset block Y range
GB_ZI = 5.9        # height of the sloped top at the inner end of the block
GB_SLOPE = 0.92    # rise of the sloped top per mm towards the wall
GB_HX = 31.15      # screw hole centre |X|
GB_HY = -49.65     # screw hole centre Y
GB_HOLE = 4.4


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------- outer body ----------------
outer = box(-HW, HW, YF, YB, 0, H)

# back right mounting tab: the side wall drops down to the tab through a
# concave sweep (profile in the YZ plane, extruded along X)
tab_block = (cq.Workplane("YZ", origin=(TAB_X0, 0, 0))
             .moveTo(YB - WT_BACK, 0)
             .lineTo(TAB_YE, 0)
             .lineTo(TAB_YE, TAB_T)
             .lineTo(YB + TAB_R, TAB_T)
             .radiusArc((YB, TAB_T + TAB_R), TAB_R)
             .lineTo(YB, H)
             .lineTo(YB - WT_BACK, H)
             .close()
             .extrude(HW - TAB_X0))
outer = outer.union(tab_block)


def edges_where(shape, test):
    """Edges of a shape whose bounding box passes the test."""
    return [e for e in shape.Edges() if test(e.BoundingBox())]


def flat(lo, hi, v):
    return abs(lo - v) < 1e-6 and abs(hi - v) < 1e-6


def round_outer(wp):
    """Big round on the front top edge, smaller round on the side top edges
    (it wraps down the front corners), small rounds along the tab sweep."""
    s = wp.val()
    s = s.fillet(R_FRONT, edges_where(
        s, lambda b: flat(b.zmin, b.zmax, H) and flat(b.ymin, b.ymax, YF)))
    s = s.fillet(R_SIDE, edges_where(
        s, lambda b: flat(b.zmin, b.zmax, H) and abs(b.xmax - b.xmin) < 1e-6
        and abs(abs(b.xmin) - HW) < 1e-6))
    s = s.fillet(R_TAB, edges_where(
        s, lambda b: flat(b.xmin, b.xmax, HW) and b.ymin > YB - 1e-6
        and b.zmin > 1e-6 and b.zmax > TAB_T + 1e-6))
    s = s.fillet(R_TAB_END, edges_where(
        s, lambda b: flat(b.ymin, b.ymax, TAB_YE) and abs(b.xmax - b.xmin) < 1e-6))
    return cq.Workplane("XY").newObject([s])


outer = round_outer(outer)

# ---------------- inner cavity (open bottom) ----------------
ri = R_FRONT - WT
side_in = (cq.Workplane("YZ", origin=(-HW + WT, 0, 0))
           .moveTo(YF + WT, -1)
           .lineTo(YF + WT, H - T - ri)
           .radiusArc((YF + WT + ri, H - T), -ri)
           .lineTo(YB - WT_BACK, H - T)
           .lineTo(YB - WT_BACK, -1)
           .close()
           .extrude(2 * (HW - WT)))
body = outer.cut(side_in)

# ---------------- U cut-out with corner lugs ----------------
cut = (cq.Workplane("XY").workplane(offset=-1)
       .moveTo(-CUT_N, YB + 2)
       .lineTo(-CUT_N, LUG_B + LUG_R)
       .radiusArc((-CUT_N - LUG_R, LUG_B), LUG_R)
       .lineTo(-CUT_W, LUG_B)
       .lineTo(-CUT_W, LUG_F)
       .lineTo(-CUT_N - LUG_R, LUG_F)
       .radiusArc((-CUT_N, LUG_F - LUG_R), LUG_R)
       .lineTo(-CUT_N, CUT_Y0)
       .lineTo(CUT_N, CUT_Y0)
       .lineTo(CUT_N, LUG_F - LUG_R)
       .radiusArc((CUT_N + LUG_R, LUG_F), LUG_R)
       .lineTo(CUT_W, LUG_F)
       .lineTo(CUT_W, LUG_B)
       .lineTo(CUT_N + LUG_R, LUG_B)
       .radiusArc((CUT_N, LUG_B + LUG_R), LUG_R)
       .lineTo(CUT_N, YB + 2)
       .close()
       .extrude(H + 2))
body = body.cut(cut)

# lug holes
for sx in (-1, 1):
    for hy in LUG_HY:
        body = body.cut(cq.Workplane("XY").workplane(offset=H - T - 0.5)
                        .center(sx * LUG_HX, hy).circle(LUG_HOLE / 2)
                        .extrude(T + 1))

# ---------------- slots through top and front wall ----------------
for sx in SLOT_X:
    body = body.cut(box(sx - SLOT_W / 2, sx + SLOT_W / 2, YF - 1, SLOT_Y1,
                        FINGER_LIFT - 0.2, H + 1))
    body = body.cut(box(sx - SLOT_W / 2, sx + SLOT_W / 2, YF - 1, YF + WT + 0.5,
                        -1, H + 1))

# raised bottom edge of the three front fingers
body = body.cut(box(SLOT_X[0], SLOT_X[3], YF - 1, YF + WT + 0.5, -1, FINGER_LIFT))

# ---------------- right side notch and window ----------------
body = body.cut(box(HW - WT, HW + 1, NOTCH_Y[0], NOTCH_Y[1], -1, H + 1))
win = (cq.Workplane("XZ", origin=(0, WIN_Y[1], 0))
       .polyline([(HW + 1, -1), (HW + 1, WIN_Z), (HW, WIN_Z),
                  (HW - WT, WIN_Z_IN), (HW - WT - 1, WIN_Z_IN),
                  (HW - WT - 1, -1)])
       .close()
       .extrude(WIN_Y[1] - WIN_Y[0]))
body = body.cut(win)

# ---------------- mounting tab hole with spot face ----------------
body = body.cut(cq.Workplane("XY").workplane(offset=-1)
                .center(TAB_HX, TAB_HY).circle(TAB_HOLE / 2).extrude(H + 2))
body = body.cut(cq.Workplane("XY").workplane(offset=TAB_T)
                .center(TAB_HX, TAB_HY).circle(TAB_CB / 2).extrude(H))

# ---------------- corner screw blocks ----------------
ceil = H - T
x_wall = HW - WT + 0.3
gb_r = (GB_Y[1] - GB_Y[0]) / 2          # half width -> round inner end
gb_yc = (GB_Y[0] + GB_Y[1]) / 2
x_in = GB_HX - gb_r                     # inner end of the rounded block
z_in = GB_ZI
x_ceil = x_in + (ceil - z_in) / GB_SLOPE
for sx in (-1, 1):
    # stadium shaped footprint, rounded around the screw hole
    foot = (cq.Workplane("XY")
            .center(GB_HX, gb_yc).circle(gb_r).extrude(ceil + 0.3)
            .union(box(GB_HX, x_wall, GB_Y[0], GB_Y[1], 0, ceil + 0.3)))
    # sloped top: keep everything under the plane rising towards the wall
    wedge = (cq.Workplane("XZ", origin=(0, GB_Y[1] + 1, 0))
             .polyline([(x_in - 1, -1), (x_wall + 1, -1), (x_wall + 1, ceil + 0.3),
                        (x_ceil, ceil + 0.3), (x_ceil, ceil),
                        (x_in - 1, z_in - GB_SLOPE)])
             .close()
             .extrude(GB_Y[1] - GB_Y[0] + 2))
    gb = foot.intersect(wedge)
    gb = gb.cut(cq.Workplane("XY").workplane(offset=-1)
                .center(GB_HX, GB_HY).circle(GB_HOLE / 2)
                .extrude(ceil - 0.6 + 1))
    if sx < 0:
        gb = gb.mirror("YZ")
    body = body.union(gb)

result = body
